import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 110.0          # overall length (X)
H = 40.0           # overall height (Z)
T = 4.5            # plate thickness (Y)
PAD_W = 16.2       # full-height end pad width
STEP_END = 22.0    # end of the shallow step, measured from the end edge
NOTCH_D = 2.6      # depth of that step (from top/bottom edge)
MID_H = 20.5       # height of the narrow middle web

HOLE_D = 7.15      # through holes in the pads
HOLE_X = 8.0       # hole centre from the end edge
HOLE_Z = 6.2       # hole centre from top/bottom edge

PIN_D = 3.15       # locating pins on the back face
PIN_L = 6.35
PIN_X = 18.6       # pin centre from the end edge
PIN_Z = 6.25       # pin centre from top/bottom edge
PIN_ROOT_R = 0.75  # root fillet
PIN_TIP_C = 0.3    # tip chamfer

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plate outline (XZ plane, thickness along +Y) ----------------
hw, hh = W / 2, H / 2
x1 = hw - PAD_W
x2 = hw - STEP_END
zn = hh - NOTCH_D
zm = MID_H / 2

pts_q = [(hw, hh), (x1, hh), (x1, zn), (x2, zn), (x2, zm)]
pts = []
pts += [(x, z) for (x, z) in pts_q]                       # right-top quadrant
pts += [(-x, z) for (x, z) in reversed(pts_q)]            # left-top
pts += [(-x, -z) for (x, z) in pts_q]                     # left-bottom
pts += [(x, -z) for (x, z) in reversed(pts_q)]            # right-bottom

# "XZ" workplane normal is -Y, so a negative extrude grows toward +Y
plate = cq.Workplane("XZ").polyline(pts).close().extrude(-T)

# four through holes in the end pads
hole_pts = [(sx * (hw - HOLE_X), sz * (hh - HOLE_Z)) for sx in (-1, 1) for sz in (-1, 1)]
cutters = None
for (hx, hz) in hole_pts:
    cyl = cq.Workplane("XZ", origin=(hx, -1.0, hz)).circle(HOLE_D / 2).extrude(-(T + 2.0))
    cutters = cyl if cutters is None else cutters.union(cyl)
plate = plate.cut(cutters)

# ---------------- locating pin (revolved profile with root fillet + tip chamfer) ----------------
r = PIN_D / 2
f = PIN_ROOT_R
c = PIN_TIP_C
k = 1 - math.sqrt(0.5)
# profile in (radius, height) on the XY plane, revolved about local Y
pin_prof = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(r + f, 0)
    .threePointArc((r + f * k, f * k), (r, f))                 # concave root fillet
    .lineTo(r, PIN_L - c)
    .lineTo(r - c, PIN_L)                                       # tip chamfer
    .lineTo(0, PIN_L)
    .close()
)
pin_solid = pin_prof.revolve(360, (0, 0, 0), (0, 1, 0)).val()
# turn the revolve seam to face -Z (underside of the pin)
pin_solid = pin_solid.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)

pin_pts = [(sx * (hw - PIN_X), sz * (hh - PIN_Z)) for sx in (-1, 1) for sz in (-1, 1)]
result = plate
for (px, pz) in pin_pts:
    result = result.union(cq.Workplane("XY").add(pin_solid.translate(cq.Vector(px, T, pz))))
